import math
import cadquery as cq

# =====================================================================
# Enclosure front shell: rounded-rectangle box, closed front face (-Y)
# with an engraved "sound bar" logo, open back (+Y) with a lid step,
# corner screw bosses, PCB standoffs tied by a rib grid, PCB guide rails,
# USB-C / button openings in the bottom wall and a slide-switch recess
# in the -X end wall.
# =====================================================================

# ---------------- overall dimensions (mm) ----------------
L = 100.0          # length along X
H = 43.0           # height along Z
D = 16.5           # depth along Y (front face at -Y, open back at +Y)
R = 8.0            # corner radius of the outline (XZ plane)
WALL = 2.4         # side wall thickness
FRONT_T = 2.0      # front wall thickness

# lid step around the open back
STEP_W = 0.9       # width of the inner step (ledge)
STEP_D = 2.0       # depth of the inner step
SO_TOP_GAP = 1.0   # standoff tips stop this far below the back rim

# logo bars engraved into the front face
BAR_W = 3.0
BAR_PITCH = 5.09
LOGO_X = 0.3       # logo centre offset along X
BAR_H = [4.8, 11.0, 17.5, 11.0, 4.8, 11.0, 17.5, 11.0, 4.8]
BAR_Z0 = -8.3      # bottom of bars
BAR_DEPTH = 0.5

# corner screw bosses
CB_X = 43.5        # half spacing along X
CB_Z = 15.0        # half spacing along Z
CB_R = 3.3
CB_HOLE = 2.4

# PCB standoffs (x, z): A, B, C, D, E
STANDOFFS = [(10.0, 9.7), (-0.8, 11.3), (-19.5, 9.7), (10.0, -9.7), (-19.5, -9.7)]
SO_R = 3.4          # standoff tip radius
SO_BASE_R = 5.6     # pillar radius below the tip
SO_CH = 2.0         # chamfer on the flange top edge
SO_FLANGE_T = 3.0   # thickness of the conical flange
SO_HOLE = 3.0

# rib grid on the floor
RIB_T = 1.2
RIB_TOP_DROP = 2.5  # rib grid top below the standoff tips
DB_RIB_Z = -12.0    # z of the rib joining standoff D to the corner block

# +X end platform and bottom corner block
PLAT_W = 9.0
PLAT_DROP = 3.2    # platform top below the standoff tips
BLK_L = 11.0
BLK_H = 8.5
BLK_FILLET = 2.0
PLAT_CH = 1.9

# -X end switch frame (rectangular ring)
FRAME_X0 = -34.5    # inner (centre side) face of the frame
FRAME_Z0 = -2.5
FRAME_Z1 = 17.5
FRAME_T = 2.2

# PCB guide rails along the bottom / top walls
RAIL_GAP = 2.0      # gap between wall and rail
RAIL_T = 2.8        # rail thickness
RAIL_CH = 2.4       # chamfer on the rail top edge
RAIL_X1 = 26.0      # +X end of the bottom rail
RAIL_DROP = 1.5     # rail top below the standoff tips

# openings
USB_X, USB_Y = 4.0, 1.5        # USB-C opening in bottom wall (centre)
USB_L, USB_W, USB_R = 9.0, 3.4, 1.1
BEZEL_L, BEZEL_W, BEZEL_H, BEZEL_R = 11.2, 6.6, 0.15, 1.6
BTN_X, BTN_Y, BTN_D = 33.7, 1.0, 6.4   # round hole in bottom wall
SW_Y, SW_Z = -0.5, -0.4         # switch recess in -X end wall
SW_L, SW_W, SW_R, SW_DEPTH = 10.4, 3.5, 1.0, 1.2
KNOB_W, KNOB_H, KNOB_OUT = 1.8, 4.0, 0.15  # slide-switch knob in the slot

VIEW = {"azimuth": 45, "elevation": 26}

# derived
X_IN = L / 2 - WALL
Z_IN = H / 2 - WALL
Y_FRONT = -D / 2
Y_BACK = D / 2
Y_FLOOR = Y_FRONT + FRONT_T
Y_TOP = Y_BACK - STEP_D          # lid ledge: top of corner bosses / corner block
Y_SO = Y_BACK - SO_TOP_GAP       # top of the PCB standoffs
Y_RIB = Y_SO - RIB_TOP_DROP      # top of the rib grid
Y_RAIL = Y_SO - RAIL_DROP        # top of the guide rails
Y_PLAT = Y_SO - PLAT_DROP        # top of the +X end platform
Y0 = Y_FLOOR - 0.5               # interior features start inside the front wall


def xz(y):
    """Workplane parallel to XZ at height y (local x = X, local y = Z, normal -Y)."""
    return cq.Workplane("XZ", origin=(0, y, 0))


def prism_y(y_lo, y_hi, sketch_fn):
    """Extrude a sketch drawn on an XZ plane from y_lo up to y_hi (+Y)."""
    return sketch_fn(xz(y_lo)).extrude(-(y_hi - y_lo))


def box_y(x0, x1, z0, z1, y_lo, y_hi):
    return prism_y(y_lo, y_hi, lambda wp: wp.center((x0 + x1) / 2, (z0 + z1) / 2)
                   .rect(abs(x1 - x0), abs(z1 - z0)))


def rounded_box(w, h, r, y_lo, y_hi):
    return prism_y(y_lo, y_hi, lambda wp: wp.rect(w, h)).edges("|Y").fillet(r)


def rib(p1, p2, t, y_lo, y_hi):
    (x1, z1), (x2, z2) = p1, p2
    dx, dz = x2 - x1, z2 - z1
    ln = math.hypot(dx, dz)
    nx, nz = -dz / ln * t / 2, dx / ln * t / 2
    pts = [(x1 + nx, z1 + nz), (x2 + nx, z2 + nz), (x2 - nx, z2 - nz), (x1 - nx, z1 - nz)]
    return prism_y(y_lo, y_hi, lambda wp: wp.polyline(pts).close())


# ---------------- outer shell ----------------
shell = rounded_box(L, H, R, Y_FRONT, Y_BACK)
shell = shell.cut(rounded_box(L - 2 * WALL, H - 2 * WALL, R - WALL, Y_FLOOR, Y_BACK + 1))
shell = shell.cut(rounded_box(L - 2 * WALL + 2 * STEP_W, H - 2 * WALL + 2 * STEP_W,
                              R - WALL + STEP_W, Y_TOP, Y_BACK + 1))

# ---------------- interior structures (clipped to the cavity) ----------------
parts = []
A, B, C, Dd, E = STANDOFFS

# corner screw bosses, tied into the corners
CORNERS = [(sx * CB_X, sz * CB_Z, sx, sz) for sx in (1, -1) for sz in (1, -1)]
for cx, cz, sx, sz in CORNERS:
    parts.append(prism_y(Y0, Y_TOP, lambda wp: wp.center(cx, cz).circle(CB_R)))
    parts.append(box_y(cx, cx + sx * 8.0, cz - CB_R, cz + CB_R, Y0, Y_TOP))
    parts.append(box_y(cx - CB_R, cx + CB_R, cz, cz + sz * 8.0, Y0, Y_TOP))

# +X end platform along the end wall, chamfered inner top edge
plat_x = X_IN - PLAT_W
plat = box_y(plat_x, X_IN + 1.0, -Z_IN - 0.5, Z_IN + 0.5, Y0, Y_PLAT)
plat = plat.faces(">Y").edges("<X").chamfer(PLAT_CH)
parts.append(plat)

# block in the bottom +X corner with a concave fillet up to the platform
blk_x0 = X_IN - BLK_L
blk_z1 = -Z_IN + BLK_H
parts.append(box_y(blk_x0, X_IN + 1.0, -Z_IN - 1.0, blk_z1, Y0, Y_TOP))
fil = box_y(plat_x - BLK_FILLET, plat_x + 0.1, blk_z1 - 0.1, blk_z1 + BLK_FILLET, Y0, Y_PLAT)
fil = fil.cut(prism_y(Y0 - 1, Y_TOP + 1, lambda wp: wp.center(plat_x - BLK_FILLET, blk_z1 + BLK_FILLET)
                      .circle(BLK_FILLET)))
parts.append(fil)

# -X end switch frame: a rectangular ring standing on the floor
frame = box_y(-X_IN - 1.0, FRAME_X0, FRAME_Z0, FRAME_Z1, Y0, Y_RAIL)
frame = frame.cut(box_y(-X_IN + FRAME_T, FRAME_X0 - FRAME_T, FRAME_Z0 + FRAME_T, FRAME_Z1 - FRAME_T,
                        Y_FLOOR + 1.0, Y_TOP + 1))
parts.append(frame)

# rib grid
rib_list = [
    ((A[0], Z_IN + 0.5), (A[0], -Z_IN - 0.5)),       # rib through A-D
    ((C[0], Z_IN + 0.5), (C[0], -Z_IN - 0.5)),       # rib through C-E
    (A, E), (C, Dd),                                  # X bracing
    ((plat_x + 0.5, A[1]), A),                        # A to +X platform
    ((plat_x - 1.0, blk_z1 + 3.0), A),                # A to corner block
    ((blk_x0 + 0.5, DB_RIB_Z), (Dd[0], DB_RIB_Z)),     # D tab to corner block
    (C, (FRAME_X0 - 0.5, C[1])),                      # C to -X frame
    (A, B), (B, C),
]
for p1, p2 in rib_list:
    parts.append(rib(p1, p2, RIB_T, Y0, Y_RIB))

# PCB guide rails parallel to the bottom and top walls (chamfered top edge)
for sz, x_lo, x_hi in ((-1, -X_IN - 1.0, RAIL_X1), (1, -X_IN - 1.0, plat_x + 0.5)):
    z_a = sz * (Z_IN - RAIL_GAP)
    z_b = sz * (Z_IN - RAIL_GAP - RAIL_T)
    rail = box_y(x_lo, x_hi, z_a, z_b, Y0, Y_RAIL)
    rail = rail.faces(">Y").edges("<Z" if sz > 0 else ">Z").chamfer(RAIL_CH)
    parts.append(rail)

# lower standoffs D, E carry tabs down to the bottom rail
z_rail = -Z_IN + RAIL_GAP + RAIL_T / 2
for (x, z) in (Dd, E):
    parts.append(box_y(x - SO_R, x + SO_R, z, z_rail, Y0, Y_SO))

# standoffs: slim post up to the lid step with a conical flange at rib level
for i, (x, z) in enumerate(STANDOFFS):
    if i == 1:
        parts.append(prism_y(Y0, Y_SO, lambda wp: wp.center(x, z).circle(SO_R)))
        continue
    pil = prism_y(Y_RIB - SO_FLANGE_T, Y_RIB, lambda wp: wp.center(x, z).circle(SO_BASE_R))
    pil = pil.faces(">Y").edges().chamfer(SO_CH)
    parts.append(pil)
    parts.append(prism_y(Y0, Y_SO, lambda wp: wp.center(x, z).circle(SO_R)))

interior = parts[0]
for p in parts[1:]:
    interior = interior.union(p)
clip = rounded_box(L - 2 * WALL + 0.4, H - 2 * WALL + 0.4, R - WALL + 0.2, Y_FLOOR - 0.2, Y_SO)
interior = interior.intersect(clip)

body = shell.union(interior)

# screw / standoff holes
for (x, z) in STANDOFFS:
    body = body.cut(prism_y(Y_FLOOR + 1.0, Y_BACK, lambda wp: wp.center(x, z).circle(SO_HOLE / 2)))
for cx, cz, sx, sz in CORNERS:
    body = body.cut(prism_y(Y_FLOOR + 1.0, Y_BACK, lambda wp: wp.center(cx, cz).circle(CB_HOLE / 2)))

# ---------------- openings ----------------
# USB-C: slightly raised rounded-rectangle bezel on the bottom face with a through opening
bezel = (
    cq.Workplane("XY", origin=(0, 0, -H / 2 + 0.5))
    .center(USB_X, USB_Y)
    .rect(BEZEL_L, BEZEL_W)
    .extrude(-(0.5 + BEZEL_H))
    .edges("|Z")
    .fillet(BEZEL_R)
)
body = body.union(bezel)
usb = (
    cq.Workplane("XY", origin=(0, 0, -H / 2 - 1.0))
    .center(USB_X, USB_Y)
    .rect(USB_L, USB_W)
    .extrude(WALL + RAIL_GAP + RAIL_T + 2.0)
    .edges("|Z")
    .fillet(USB_R)
)
body = body.cut(usb)

# round hole in the bottom wall
btn = (
    cq.Workplane("XY", origin=(0, 0, -H / 2 - 1.0))
    .center(BTN_X, BTN_Y)
    .circle(BTN_D / 2)
    .extrude(WALL + 4.0)
)
body = body.cut(btn)

# switch recess in the -X end wall (long axis along Z)
sw = (
    cq.Workplane("YZ", origin=(-L / 2 - 1.0, 0, 0))
    .center(SW_Y, SW_Z)
    .rect(SW_W, SW_L)
    .extrude(1.0 + SW_DEPTH)
    .edges("|X")
    .fillet(SW_R)
)
body = body.cut(sw)
# slide-switch knob sitting in the recess, just proud of the end face
knob = (
    cq.Workplane("YZ", origin=(-L / 2 - KNOB_OUT, 0, 0))
    .center(SW_Y, SW_Z)
    .rect(KNOB_W, KNOB_H)
    .extrude(KNOB_OUT + SW_DEPTH + 0.1)
)
body = body.union(knob)

# ---------------- logo bars ----------------
n = len(BAR_H)
x0 = LOGO_X - (n - 1) / 2 * BAR_PITCH
for i, bh in enumerate(BAR_H):
    bx = x0 + i * BAR_PITCH
    bz = BAR_Z0 + bh / 2
    body = body.cut(xz(Y_FRONT).center(bx, bz).rect(BAR_W, bh).extrude(-BAR_DEPTH))

result = body
